import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Maze-ring puzzle: seven loose grooved rings with wire patterns, plus a
# stand (tower) holding a stack of seven rings on four posts, a base hoop,
# a pyramid + ball pedestal and four claw feet.
# ---------------------------------------------------------------------------

# ring dimensions
RO = 15.0          # ring outer radius
RI = 12.9          # ring inner radius
RT = 1.95          # loose ring thickness (height)
STACK_RT = 2.3     # stacked ring thickness
GROOVE_D = 0.22    # depth of the groove between the two rim beads
RIM_INSET = 0.12   # inset of the rim at the top / bottom faces
CREST_GAP = 0.02   # crest of the beads sits just inside RO
STACK_EDGE_R = 1.05   # rounding of the rim of the stacked rings

# wire (bar) pattern inside the ring
BAR_W = 0.5
BAR_H = 0.7
ATTACH_R = 0.91    # normalised radius used when a bar end attaches to the ring

# tower (stand)
STACK_N = 7
STACK_PITCH = 3.48
STACK_BOTTOM = 21.4        # z of bottom face of lowest ring
POST_R = 1.5
POST_PR = 14.2             # radial position of posts
LUG_R = 2.0                # lugs of the top stacked ring around the posts
LUG_FILLET = 0.25
HOOP_R = 14.1              # base torus major radius
HOOP_TUBE = 1.75           # base torus tube radius
HOOP_Z = 5.06
PYR_A = 10.0               # pyramid half diagonal (corners on X / Y axes)
PYR_AT = 0.3               # half diagonal of the (almost pointed) top
PYR_ZB = 5.8
PYR_ZT = 10.5
BALL_R = 4.3
BALL_Z = 16.2
NECK_SLACK = 2.0          # degrees the funnel is narrower than tangent
SPOKE_R = 1.55
FOOT_ROOT_R = 17.3
FOOT_ROOT_Z = 5.3
FOOT_TIP_R = 19.8
FOOT_BASE_R = 1.1
FOOT_STUB_R = 0.9

# wire patterns, normalised to RO, +Y up in top view
PATTERNS = {
    "A": [
        [(-0.69, 0.53), (-0.38, 0.20), (-0.36, -0.02), (-0.54, -0.02),
         (-0.63, -0.15), (-0.62, -0.55), (0.65, -0.55)],
    ],
    "B": [
        [(-0.62, 0.67), (0.62, 0.67)],
        [(-0.57, 0.67), (-0.57, 0.22), (-0.88, 0.22)],
        [(-0.88, -0.17), (-0.50, -0.22), (0.0, -0.88), (0.48, -0.26)],
    ],
    "C": [
        [(-1.0, 0.20), (1.0, 0.20)],
        [(-1.0, -0.20), (1.0, -0.20)],
    ],
    "D": [
        [(-0.52, -0.70), (-0.39, -0.02), (-0.57, 0.04), (-0.54, 0.17),
         (-0.37, 0.26), (-0.26, 0.80)],
        [(-0.12, 0.85), (0.28, 0.15), (0.46, 0.70)],
    ],
    "E": [
        [(0.50, 0.74), (0.48, -0.15), (0.35, -0.28), (0.74, -0.52)],
        [(0.35, -0.28), (-0.13, -0.86)],
        [(-0.13, -0.86), (-0.33, 0.15), (-0.17, 0.15), (-0.17, 0.01),
         (-0.31, 0.0)],
        [(-0.27, 0.0), (-0.09, -0.22), (0.42, -0.22)],
    ],
    "F": [
        [(-0.55, 0.70), (0.15, 0.80)],
        [(-0.55, 0.70), (0.0, 0.15), (0.0, -0.22), (0.26, -0.22),
         (0.26, 0.17), (0.52, 0.22), (0.80, 0.43)],
    ],
    "G": [
        [(-0.51, -0.70), (-0.18, -0.25), (0.42, -0.70)],
        [(0.42, -0.70), (0.62, -0.45), (0.62, -0.05), (0.80, -0.05)],
        [(0.62, -0.05), (0.62, 0.12), (0.80, 0.12)],
        [(0.62, 0.12), (0.62, 0.30), (0.42, 0.78)],
    ],
}

# loose ring placement (x, y, z of ring mid plane)
LOOSE = {
    "A": (-196.8, -14.0, 88.7),
    "B": (-148.0, -14.0, 94.0),
    "C": (-91.6, -14.0, 54.3),
    "D": (-214.6, -80.0, 38.3),
    "E": (-158.2, -77.0, 33.1),
    "F": (-102.4, -75.6, 27.8),
    "G": (-48.1, -76.0, 22.4),
}

STACK_ORDER = ["G", "F", "E", "D", "B", "A", "C"]   # bottom -> top


def bead_crest(h):
    """Height of the crest of a bead arc running from (RO-RIM_INSET, h) to
    (RO-GROOVE_D, 0) whose outermost point lies at r = RO - CREST_GAP."""
    a, g = RIM_INSET - CREST_GAP, GROOVE_D - CREST_GAP

    def diff(zm):
        return (a * a + (h - zm) ** 2) / (2 * a) - (g * g + zm * zm) / (2 * g)

    lo, hi = 0.0, h
    for _ in range(60):
        mid = 0.5 * (lo + hi)
        if diff(lo) * diff(mid) <= 0:
            hi = mid
        else:
            lo = mid
    return 0.5 * (lo + hi)


def ring_body(grooved=True, t=RT):
    """Flat ring, centred on origin, mid plane at z=0.

    An extruded annulus whose outer rim is shaped by a revolved cutter
    (seam turned to +Y): loose rings get two flat convex beads meeting in a
    groove round the middle, the stacked rings of the stand a rounded rim.
    """
    h = t / 2.0
    body = (cq.Workplane("XY").circle(RO).circle(RI).extrude(t)
            .rotate((0, 0, 0), (0, 0, 1), -45)
            .translate((0, 0, -h)))
    e = 0.5
    cut = (cq.Workplane("XZ")
           .moveTo(RO + e, -h - e)
           .lineTo(RO + e, h + e))
    if grooved:
        zm = bead_crest(h)
        cut = (cut.lineTo(RO - RIM_INSET, h + e)
               .lineTo(RO - RIM_INSET, h)
               .threePointArc((RO - CREST_GAP, zm), (RO - GROOVE_D, 0.0))
               .threePointArc((RO - CREST_GAP, -zm), (RO - RIM_INSET, -h))
               .lineTo(RO - RIM_INSET, -h - e))
    else:
        f = STACK_EDGE_R
        k = 1.0 - 1.0 / math.sqrt(2.0)
        cut = (cut.lineTo(RO - f, h + e)
               .lineTo(RO - f, h)
               .threePointArc((RO - f * k, h - f * k), (RO, h - f))
               .lineTo(RO, -h + f)
               .threePointArc((RO - f * k, -h + f * k), (RO - f, -h))
               .lineTo(RO - f, -h - e))
    cutter = (cut.close().revolve(360, (0, 0, 0), (0, 1, 0))
              .rotate((0, 0, 0), (0, 0, 1), 90))
    return body.cut(cutter)


def bar(p1, p2, t=RT):
    x1, y1 = p1
    x2, y2 = p2
    L = math.hypot(x2 - x1, y2 - y1)
    ang = math.degrees(math.atan2(y2 - y1, x2 - x1))
    return (cq.Workplane("XY")
            .box(L + BAR_W, BAR_W, BAR_H)
            .rotate((0, 0, 0), (0, 0, 1), ang)
            .translate(((x1 + x2) / 2, (y1 + y2) / 2, t / 2 - BAR_H / 2)))


def snap(p):
    """Points close to the rim are pushed into the ring wall."""
    r = math.hypot(p[0], p[1])
    if r > 0.75:
        return (p[0] / r * ATTACH_R * RO, p[1] / r * ATTACH_R * RO)
    return (p[0] * RO, p[1] * RO)


def pattern_ring(key, stacked=False):
    t = STACK_RT if stacked else RT
    body = ring_body(grooved=not stacked, t=t)
    bars = None
    for path in PATTERNS[key]:
        pts = [snap(p) for p in path]
        for a, b in zip(pts[:-1], pts[1:]):
            s = bar(a, b, t)
            bars = s if bars is None else bars.union(s)
    clip = cq.Workplane("XY").circle(RI + 0.6).extrude(t).translate((0, 0, -t / 2))
    bars = bars.intersect(clip)
    return body.union(bars)


def claw(angle_deg):
    """Ogive-shaped spike foot with a rounded knuckle, leaning outwards."""
    a = math.radians(angle_deg)
    c, s = math.cos(a), math.sin(a)
    root = cq.Vector(FOOT_ROOT_R * c, FOOT_ROOT_R * s, FOOT_ROOT_Z)
    tip = cq.Vector(FOOT_TIP_R * c, FOOT_TIP_R * s, 0.0)
    L = (tip - root).Length
    lean = math.degrees(math.atan2(FOOT_TIP_R - FOOT_ROOT_R, FOOT_ROOT_Z))
    r0 = FOOT_BASE_R
    # profile in the XZ plane, spike pointing down along -Z from the origin
    prof = (cq.Workplane("XZ")
            .moveTo(0, r0)
            .threePointArc((r0, 0), (r0 * 0.97, -L * 0.25))
            .threePointArc((r0 * 0.72, -L * 0.62), (0.05, -L))
            .lineTo(0, -L)
            .close())
    spike = prof.revolve(360, (0, 0, 0), (0, 1, 0))
    spike = (spike.rotate((0, 0, 0), (0, 1, 0), -lean)
             .rotate((0, 0, 0), (0, 0, 1), angle_deg)
             .translate(root))
    # short stub joining the knuckle to the base hoop
    stub = (cq.Workplane("YZ").circle(FOOT_STUB_R).extrude(FOOT_ROOT_R - HOOP_R)
            .translate((HOOP_R, 0, FOOT_ROOT_Z))
            .rotate((0, 0, 0), (0, 0, 1), angle_deg))
    return spike.union(stub)


def tower():
    # stacked rings; the top one has four lugs wrapping round the post heads
    t = None
    for i, key in enumerate(STACK_ORDER):
        zc = STACK_BOTTOM + STACK_RT / 2 + i * STACK_PITCH
        r = pattern_ring(key, stacked=True)
        for k in (range(4) if i == STACK_N - 1 else []):
            a = math.radians(90 * k)
            lug = (cq.Workplane("XY").circle(LUG_R).extrude(STACK_RT)
                   .edges().fillet(LUG_FILLET)
                   .rotate((0, 0, 0), (0, 0, 1), 90 * k + 180)
                   .translate((POST_PR * math.cos(a), POST_PR * math.sin(a), -STACK_RT / 2)))
            r = r.union(lug)
        r = r.translate((0, 0, zc))
        t = r if t is None else t.union(r)
    top = STACK_BOTTOM + STACK_RT + (STACK_N - 1) * STACK_PITCH

    # posts
    for k in range(4):
        a = math.radians(90 * k)
        p = (cq.Workplane("XY").circle(POST_R).extrude(top - HOOP_Z)
             .rotate((0, 0, 0), (0, 0, 1), 90 * k + 180)
             .translate((POST_PR * math.cos(a), POST_PR * math.sin(a), HOOP_Z)))
        t = t.union(p)

    # spokes along X and Y
    for k in range(2):
        sp = (cq.Workplane("YZ").circle(SPOKE_R).extrude(HOOP_R, both=True)
              .translate((0, 0, HOOP_Z + 0.2)))
        if k:
            sp = sp.rotate((0, 0, 0), (0, 0, 1), 90)
        t = t.union(sp)

    # pyramid (corners on the X / Y axes)
    pyr = (cq.Workplane("XY").workplane(offset=PYR_ZB)
           .rect(PYR_A * math.sqrt(2), PYR_A * math.sqrt(2))
           .workplane(offset=PYR_ZT - PYR_ZB).rect(PYR_AT * math.sqrt(2), PYR_AT * math.sqrt(2))
           .loft().rotate((0, 0, 0), (0, 0, 1), 45))
    t = t.union(pyr)

    # ball on a short neck
    ball = cq.Workplane("XY").sphere(BALL_R).translate((0, 0, BALL_Z))
    # conical funnel from the pyramid tip, (almost) tangent to the ball
    apex = PYR_ZT - 0.6                      # virtual apex of the funnel
    d = BALL_Z - apex
    half = math.asin(BALL_R / d) - math.radians(NECK_SLACK)
    z0 = apex + 0.3
    z1 = apex + d - BALL_R * BALL_R / d        # height of the tangent circle
    r0 = (z0 - apex) * math.tan(half)
    r1 = (z1 - apex) * math.tan(half)
    neck = cq.Workplane("XY").add(
        cq.Solid.makeCone(r0, r1, z1 - z0, cq.Vector(0, 0, z0), cq.Vector(0, 0, 1)))
    t = t.union(ball).union(neck)

    # base hoop (torus) + claw feet; unified without face merging, which
    # upsets the toroidal faces
    hoop = cq.Workplane("XY").add(
        cq.Solid.makeTorus(HOOP_R, HOOP_TUBE, cq.Vector(0, 0, HOOP_Z), cq.Vector(0, 0, 1))
    ).rotate((0, 0, 0), (0, 0, 1), 90)
    t = t.union(hoop, clean=False)
    for k in range(4):
        t = t.union(claw(90 * k), clean=False)
    return t


# ---------------------------------------------------------------------------
# assemble: the stand plus the seven loose rings, kept as separate solids
# ---------------------------------------------------------------------------
parts = [tower()]
for key, (x, y, z) in LOOSE.items():
    parts.append(pattern_ring(key).translate((x, y, z)))

solids = [sol for p in parts for sol in p.solids().vals()]
result = cq.Workplane("XY").add(cq.Compound.makeCompound(solids))

VIEW = {"azimuth": 45, "elevation": 26}
